import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 50.0        # outer radius of the rim shell
T_SHELL = 0.4       # rim shell thickness
LENGTH = 40.0       # axial length (along Y)

R_HUB_O = 18.75     # hub outer radius
R_HUB_I = 15.6      # hub bore radius at the front lip
R_HUB_CB = 17.6     # hub counterbore radius (from the back end)
LIP_LEN = 2.0       # axial length of the front bore lip
HUB_RECESS = 8.0    # axial recess of the hub faces from each rim end

N_CELLS = 10        # number of keyhole cells
R_BULB = 7.5        # bulb (round end) inner radius
T_WALL = 0.5        # cell wall thickness
W_NECK_HUB = 1.55   # inner half width of the neck at the hub
W_NECK_TOP = 4.1    # inner half width of the neck at the shoulder
R_SHOULDER = 33.3   # radius where the neck line ends and the shoulder starts
BULB_JOIN = 220.0   # polar angle (deg, about the bulb centre) where the shoulder joins the bulb

R_CONE_START = 32.4 # radius where the conical recess starts at the rim plane
R_CONE_END = 26.0   # radius where the recess cone reaches the hub-face depth

R_BULB_C = R_OUT - T_WALL - R_BULB - 0.05  # bulb centre radius (bulb wall merges into rim)
Y_SPLIT = LENGTH / 2.0 - HUB_RECESS         # cells are built in three axial sections

VIEW = {"azimuth": 45, "elevation": 26}


def keyhole_face(d=0.0):
    """2D keyhole cell section in a local plane, axis along +y.

    One smooth interpolating spline: straight tapered neck from the hub,
    concave shoulder, round bulb and back down the other side of the neck;
    closed by a short straight bottom that stays buried in the hub wall.
    d > 0 grows the profile outward by d (outer skin of the wall).
    """
    r0 = R_HUB_CB + T_WALL + 0.3  # neck root (buried in the hub wall)
    slope = (W_NECK_TOP - W_NECK_HUB) / (R_SHOULDER - R_HUB_O)
    ln = math.hypot(slope, 1.0)
    nx, ny = -1.0 / ln, -slope / ln   # outward normal of the left neck line
    tx, ty = -slope / ln, 1.0 / ln    # left neck direction (outward)

    def neck_pt(r):
        w = W_NECK_HUB + slope * (r - R_HUB_O)
        return (-w + d * nx, r + d * ny)

    rs = [r0 + (R_SHOULDER - r0) * i / 5.0 for i in range(6)]
    pts = [neck_pt(r) for r in rs]
    tans = [(tx, ty)] * len(rs)
    # round the bulb (clockwise about its centre), unit tangents of the circle
    for a in [BULB_JOIN, 180.0, 150.0, 120.0, 90.0, 60.0, 30.0, 0.0, 180.0 - BULB_JOIN]:
        ar = math.radians(a)
        pts.append(((R_BULB + d) * math.cos(ar), R_BULB_C + (R_BULB + d) * math.sin(ar)))
        tans.append((math.sin(ar), -math.cos(ar)))
    for r in reversed(rs):
        x, y = neck_pt(r)
        pts.append((-x, y))
        tans.append((tx, -ty))
    # unit tangents + chord-length parameters -> no scaling (keeps it fair)
    spl = cq.Edge.makeSpline(
        [cq.Vector(x, y, 0) for x, y in pts],
        tangents=[cq.Vector(a, b, 0) for a, b in tans],
        scale=False,
    )
    bottom = cq.Edge.makeLine(cq.Vector(pts[-1][0], pts[-1][1], 0), cq.Vector(pts[0][0], pts[0][1], 0))
    return cq.Face.makeFromWires(cq.Wire.assembleEdges([spl, bottom]))


def place(s, y_start):
    """local sketch (x, y) -> global (X, Z); local +z extrusion -> global -Y."""
    s = s.translate(cq.Vector(0, 0, -y_start))
    return s.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), 90)


def extrude_y(face, y_a, y_b):
    """extrude a local keyhole face so that it spans global Y = y_a .. y_b."""
    return place(cq.Solid.extrudeLinear(face, cq.Vector(0, 0, y_b - y_a)), y_b)


def cell_wall(cut_f, cut_b):
    """thin keyhole wall over the full length, ends trimmed by the recesses.

    The outer skin is one extrusion; the cavity is cut in three axial steps
    (the cavity faces therefore stay split at the hub-face depth).
    """
    fin = keyhole_face(0.0)
    fout = keyhole_face(T_WALL)
    over = 1.0  # cutter overrun past the end planes
    wall = extrude_y(fout, -LENGTH / 2.0, LENGTH / 2.0)
    wall = wall.cut(extrude_y(fin, -Y_SPLIT, Y_SPLIT))
    wall = wall.cut(extrude_y(fin, -LENGTH / 2.0 - over, -Y_SPLIT))
    wall = wall.cut(extrude_y(fin, Y_SPLIT, LENGTH / 2.0 + over))
    return wall.cut(cut_f).cut(cut_b)


def tube(r_o, r_i, y_a, y_b):
    """coaxial tube on the Y axis spanning Y = y_a .. y_b."""
    return (
        cq.Workplane("XZ", origin=(0, y_b, 0))
        .circle(r_o)
        .circle(r_i)
        .extrude(y_b - y_a)
        .val()
    )


# ---- conical + flat recess at both ends (cone flank, flat floor at the hub face)
k = (R_CONE_START - R_CONE_END) / HUB_RECESS   # radial run per mm of depth
y0 = -LENGTH / 2.0
r_top = R_CONE_START + 1.0 * k
r_bot = R_CONE_END
cut_front = cq.Solid.makeCone(
    r_top, r_bot, HUB_RECESS + 1.0, cq.Vector(0, y0 - 1.0, 0), cq.Vector(0, 1, 0)
)
cut_back = cq.Solid.makeCone(
    r_top, r_bot, HUB_RECESS + 1.0, cq.Vector(0, -y0 + 1.0, 0), cq.Vector(0, -1, 0)
)

# ---- one cell wall (patterned below)
cell = cell_wall(cut_front, cut_back)

# ---- hub: front lip + counterbore from the back
hub = tube(R_HUB_O, R_HUB_I, -Y_SPLIT, -Y_SPLIT + LIP_LEN).fuse(
    tube(R_HUB_O, R_HUB_CB, -Y_SPLIT + LIP_LEN, Y_SPLIT)
).clean()

# ---- rim shell (seam turned to the hidden lower-left side)
shell = tube(R_OUT, R_OUT - T_SHELL, -LENGTH / 2.0, LENGTH / 2.0).rotate(
    cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 130
)
# hub seams at the bottom of the bore
hub = hub.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 90)


def polar(shape, i):
    """i-th copy of the circular pattern about the Y axis."""
    return shape.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), i * 360.0 / N_CELLS)


body = shell.fuse(hub)
for i in range(N_CELLS):
    body = body.fuse(polar(cell, i))
# merge the coplanar / coaxial faces left by the booleans
body = body.clean()

solids = body.Solids()
result = cq.Workplane("XY").add(solids[0] if len(solids) == 1 else body)
